import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
from OCP.TColgp import TColgp_Array1OfPnt2d
from OCP.gp import gp_Pnt2d

# =====================================================================
#  Standard six-sided die (pips: 1 top, 6 bottom, 3 front, 4 back,
#  5 right, 2 left), cube body with edge rounds that are tight along
#  the edges and open up into ball-like rounded corners.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
EDGE = 16.0                 # cube edge length
A = EDGE / 2.0              # half edge
R_MID = 0.05 * A            # edge round radius at the middle of each edge
R_END = 0.30 * A            # edge round radius at the corners (ball-like corners)
T_FLAT = 0.35               # fraction of the half-edge kept at R_MID before growing
LAW_PTS = 21                # samples of the radius law along each edge

PIP_OFF = 0.5 * A           # pip offset from face centre (both directions)
PIP_R = 0.212 * A           # pip radius at the face
PIP_DEPTH = 0.35 * PIP_R    # pip (spherical dimple) depth

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- body: cube with variable-radius edge rounds ----------------
def round_law(n=LAW_PTS):
    """(normalised edge parameter, radius) pairs: R_MID at mid-edge, growing
    smoothly (smoothstep, zero slope at both ends) to R_END at the corners."""
    law = []
    for i in range(n):
        u = i / (n - 1.0)
        t = abs(2.0 * u - 1.0)                      # 0 at mid-edge, 1 at a corner
        s = min(1.0, max(0.0, (t - T_FLAT) / (1.0 - T_FLAT)))
        law.append((u, R_MID + (R_END - R_MID) * s * s * (3.0 - 2.0 * s)))
    return law


def variable_round(solid, law):
    """Variable-radius fillet on every edge of the solid."""
    mk = BRepFilletAPI_MakeFillet(solid.wrapped)
    for e in solid.Edges():
        arr = TColgp_Array1OfPnt2d(1, len(law))
        for i, (u, r) in enumerate(law):
            arr.SetValue(i + 1, gp_Pnt2d(u, r))
        mk.Add(arr, e.wrapped)
    mk.Build()
    return cq.Shape.cast(mk.Shape())


cube = cq.Workplane("XY").box(EDGE, EDGE, EDGE)
try:
    rounded = variable_round(cube.val(), round_law())
    if not rounded.isValid():
        raise ValueError("variable round failed")
    body = cq.Workplane("XY").add(rounded)
except Exception:
    # fallback: constant round of the mean radius
    body = cube.edges().fillet(0.5 * (R_MID + R_END))

# ---------------- pips: spherical dimples ----------------
RS = (PIP_R ** 2 + PIP_DEPTH ** 2) / (2.0 * PIP_DEPTH)   # dimple sphere radius
CO = A + RS - PIP_DEPTH                                  # sphere centre distance from die centre

d = PIP_OFF
# pip centres in face coordinates
#   +Z (top)    : 1  (x, y)
#   -Z (bottom) : 6  (x, y)  two rows x = +-d, three pips along y
#   -Y (front)  : 3  (x, z)  diagonal lower-left -> upper-right
#   +Y (back)   : 4  (x, z)
#   +X (right)  : 5  (y, z)
#   -X (left)   : 2  (y, z)  diagonal
faces = {
    "+Z": [(0.0, 0.0)],
    "-Z": [(x, y) for x in (-d, d) for y in (-d, 0.0, d)],
    "-Y": [(t, t) for t in (-d, 0.0, d)],
    "+Y": [(x, z) for x in (-d, d) for z in (-d, d)],
    "+X": [(y, z) for y in (-d, d) for z in (-d, d)] + [(0.0, 0.0)],
    "-X": [(t, t) for t in (-d, d)],
}


def pip_cutter(face, u, v):
    """Spherical dimple cutter; the primitive's seam (local +X) is turned to
    face away from the die so it never crosses the dimple surface."""
    s = cq.Solid.makeSphere(RS, angleDegrees1=-90, angleDegrees2=90)
    if face == "+X":
        c = (CO, u, v)
    elif face == "-X":
        s = s.rotate((0, 0, 0), (0, 0, 1), 180)
        c = (-CO, u, v)
    elif face == "+Y":
        s = s.rotate((0, 0, 0), (0, 0, 1), 90)
        c = (u, CO, v)
    elif face == "-Y":
        s = s.rotate((0, 0, 0), (0, 0, 1), -90)
        c = (u, -CO, v)
    elif face == "+Z":
        s = s.rotate((0, 0, 0), (0, 1, 0), -90)
        c = (u, v, CO)
    else:  # "-Z"
        s = s.rotate((0, 0, 0), (0, 1, 0), 90)
        c = (u, v, -CO)
    return s.translate(cq.Vector(*c))


result = body
for face, pts in faces.items():
    for (u, v) in pts:
        result = result.cut(cq.Workplane("XY").add(pip_cutter(face, u, v)))
